import math
import cadquery as cq

# ---------------------------------------------------------------------------
# Driving dimensions (mm).  Ring centre at the origin, part lies on z = 0..T
# ---------------------------------------------------------------------------
T = 9.17           # overall thickness
RO = 16.5          # ring outer radius
RI = 12.1          # ring bore radius

# side block (cable-tie lug) in front-left of the ring
BX_L = -31.0       # left face x
BY_F = -12.8       # front face y
BY_T = 1.9         # back face y of the block
BR = 8.8           # back-left corner radius of the block

# arm (spring finger) leaving the ring towards back-left
ARM_ANG = 130.8    # direction of the arm (deg from +X)
W_R = 0.58         # right edge offset from a radial line through the centre
W_L = -5.54        # left edge offset (arm width = W_R - W_L)
TIP_X = -26.46     # tip end face (normal -X)
TIP_Y = 29.5       # tip end face (normal +Y)
X_V = -16.32       # straight flank running up from the block
R_F = 14.42        # blend radius between that flank and the arm
CH = 1.8           # chamfer on the arm outer edge and on the tip
TIP_DR = 0.7       # draft set-back of the tip end face at the top

# cable-tie pocket (top and bottom) + through opening
P_XL = -27.46      # pocket left wall x
P_XR_F = -19.32    # pocket right wall x at the front face
P_XR_B = -23.1     # pocket right wall x at the back of the pocket
P_YB = -5.2        # back of the pocket
P_CR_L = 1.25      # back-left corner radius of the pocket
P_CR_R = 1.6       # back-right corner radius of the pocket
ND = 2.47          # notch depth (top and bottom)
NF_L = 1.5         # fillet at notch floor, left wall
NF_R = 1.1         # fillet at notch floor, right wall / back
H_R = 3.1          # radius of the through opening at mid height
H_X = (P_XL + P_XR_B) / 2.0
H_Y = P_YB

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------------------------------------------------------------------
# helpers
# ---------------------------------------------------------------------------
ua = (math.cos(math.radians(ARM_ANG)), math.sin(math.radians(ARM_ANG)))
nr = (ua[1], -ua[0])          # outward normal of the arm's right edge


def on_right_edge_y(y):
    # x on the right edge line for given y
    return (W_R - nr[1] * y) / nr[0]


def on_left_edge_x(x):
    # y on the left edge line for given x
    return (W_L - nr[0] * x) / nr[1]


# ---------------------------------------------------------------------------
# ring
# ---------------------------------------------------------------------------
ring = cq.Workplane("XY").circle(RO).extrude(T)

# ---------------------------------------------------------------------------
# block
# ---------------------------------------------------------------------------
BX_R = -10.0
block = (
    cq.Workplane("XY")
    .moveTo(BX_L, BY_F)
    .lineTo(BX_R, BY_F)
    .lineTo(BX_R, BY_T)
    .lineTo(BX_L + BR, BY_T)
    .radiusArc((BX_L, BY_T - BR), -BR)
    .close()
    .extrude(T)
)

# ---------------------------------------------------------------------------
# arm
# ---------------------------------------------------------------------------
# blend arc centre (tangent to x = X_V and to the arm left edge)
cx = X_V - R_F
cy = (W_L - R_F - nr[0] * cx) / nr[1]
p_tan = (cx + R_F * nr[0], cy + R_F * nr[1])       # tangent point on left edge
a0 = 0.0
a1 = math.atan2(p_tan[1] - cy, p_tan[0] - cx)
am = 0.5 * (a0 + a1)
p_mid = (cx + R_F * math.cos(am), cy + R_F * math.sin(am))

p_tipL = (TIP_X, on_left_edge_x(TIP_X))
p_tipC = (TIP_X, TIP_Y)
p_tipR = (on_right_edge_y(TIP_Y), TIP_Y)
# deep point on the right edge, inside the ring wall
d_in = RO - 2.0
# point on right edge line at distance d_in from the origin (towards tip)
# param: p = W_R*nr + t*ua ; |p|^2 = W_R^2 + t^2
t_in = math.sqrt(d_in ** 2 - W_R ** 2)
p_in = (W_R * nr[0] + t_in * ua[0], W_R * nr[1] + t_in * ua[1])

arm = (
    cq.Workplane("XY")
    .moveTo(X_V, BY_T - 1.0)
    .lineTo(X_V, cy)
    .threePointArc(p_mid, p_tan)
    .lineTo(*p_tipL)
    .lineTo(*p_tipC)
    .lineTo(*p_tipR)
    .lineTo(*p_in)
    .lineTo(-12.0, BY_T - 1.0)
    .close()
    .extrude(T)
)


def _mid_box(p, q, z, tol=0.3):
    mx, my = 0.5 * (p[0] + q[0]), 0.5 * (p[1] + q[1])
    return cq.selectors.BoxSelector((mx - tol, my - tol, z - tol),
                                    (mx + tol, my + tol, z + tol))


sel = None
for z in (0.0, T):
    for (p, q) in ((p_tipC, p_tipR), (p_tipR, p_in)):
        s = _mid_box(p, q, z)
        sel = s if sel is None else (sel + s)
arm = arm.edges(sel).chamfer(CH)

# ---------------------------------------------------------------------------
# union + bore
# ---------------------------------------------------------------------------
body = ring.union(block).union(arm)
body = body.cut(cq.Workplane("XY").circle(RI).extrude(T))

# slight draft on the tip end face (top edge set back by TIP_DR)
tip_wedge = (
    cq.Workplane("XZ", origin=(0, TIP_Y + 5.0, 0))
    .polyline([
        (TIP_X - TIP_DR / T, -1.0),
        (TIP_X + TIP_DR * (T + 1.0) / T, T + 1.0),
        (TIP_X - 10.0, T + 1.0),
        (TIP_X - 10.0, -1.0),
    ])
    .close()
    .extrude(15.0)
)
body = body.cut(tip_wedge)

# ---------------------------------------------------------------------------
# cable-tie pockets
# ---------------------------------------------------------------------------
y_front = BY_F - 2.0
slope = (P_XR_F - P_XR_B) / (BY_F - P_YB)
x_rf = P_XR_B + slope * (y_front - P_YB)


def pocket_prism(z0, h):
    w = (
        cq.Workplane("XY")
        .workplane(offset=z0)
        .moveTo(P_XL, y_front)
        .lineTo(x_rf, y_front)
        .lineTo(P_XR_B, P_YB)
        .lineTo(P_XL, P_YB)
        .close()
        .extrude(h)
    )
    w = w.edges("|Z").edges(cq.selectors.BoxSelector(
        (P_XL - 0.3, P_YB - 0.3, z0 - 1), (P_XL + 0.3, P_YB + 0.3, z0 + h + 1))
    ).fillet(P_CR_L)
    w = w.edges("|Z").edges(cq.selectors.BoxSelector(
        (P_XR_B - 0.3, P_YB - 0.3, z0 - 1), (P_XR_B + 0.3, P_YB + 0.3, z0 + h + 1))
    ).fillet(P_CR_R)
    return w


top_cut = pocket_prism(T - ND, ND + 1.0)
bot_cut = pocket_prism(-1.0, ND + 1.0)

# through opening: revolved profile with a full round on the bridge edge
rb = (T - 2 * ND) / 2.0
R1 = H_R + rb
zb, zt = ND, T - ND
rev = (
    cq.Workplane("XZ")
    .moveTo(0, -1.0)
    .lineTo(R1, -1.0)
    .lineTo(R1, zb)
    .threePointArc((R1 - rb, T / 2.0), (R1, zt))
    .lineTo(R1, T + 1.0)
    .lineTo(0, T + 1.0)
    .close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
    .translate((H_X, H_Y, 0))
)
through = rev.intersect(pocket_prism(-1.0, T + 2.0))

body = body.cut(top_cut).cut(bot_cut).cut(through)

# round the pocket floor / bridge nose into the side walls (one tangent chain
# per wall: top floor -> round nose -> bottom floor)
_rx1, _ry1, _rx2, _ry2 = P_XR_F, BY_F, P_XR_B, P_YB
_rl = math.hypot(_rx2 - _rx1, _ry2 - _ry1)


def _in_bridge(c):
    return BY_F + 0.05 < c.y < P_YB - 1.5 and 0.5 < c.z < T - 0.5


def _left_chain(e):
    c = e.Center()
    return abs(c.x - P_XL) < 0.05 and _in_bridge(c) and not (
        e.geomType() == "LINE" and abs(c.z - T / 2.0) < 0.01)


def _right_chain(e):
    c = e.Center()
    d = abs((_rx2 - _rx1) * (_ry1 - c.y) - (_rx1 - c.x) * (_ry2 - _ry1)) / _rl
    return d < 0.05 and _in_bridge(c) and not (
        e.geomType() == "LINE" and abs(c.z - T / 2.0) < 0.01)


solid = body.val()
for _rad, _pick in ((NF_L, _left_chain), (NF_R, _right_chain)):
    _edges = [e for e in solid.Edges() if _pick(e)]
    if _edges:
        try:
            _s = solid.fillet(_rad, _edges)
            if _s.isValid():
                solid = _s
        except Exception:
            pass

result = cq.Workplane("XY").add(solid)
